import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 100.0        # outer radius of pulley
T = 13.8             # disc / rim thickness
GROOVE_R = 5.15      # radius of the round belt groove
SPOKE_W = 40.0       # width of the cross spokes
CUT_R = 82.3         # outer radius of the window cut-outs
CUT_FILLET_IN = 3.0  # window fillet at the corner next to the hub
CUT_FILLET_OUT = 3.5 # window fillets where the straight sides meet the arc
HUB_D = 26.6         # hub boss diameter
HUB_H = 12.4         # hub height above top face
HUB_FILLET = 2.0     # fillet at hub base
HUB_CHAMFER = 0.0    # chamfer at hub top edge
SPL_MAJOR = 21.2     # spline bore major diameter
SPL_MINOR = 19.0     # spline bore minor diameter
SPL_TEETH = 24       # number of spline teeth
SPL_DEPTH = HUB_H + 4.0  # depth of the spline bore from hub top
HOLE_D = 8.6         # small through hole
SEAM_ANGLE = 150.0   # angular position of the revolve seam (cosmetic)

# ---------------- revolved body: disc + groove + hub ----------------
rh = HUB_D / 2
f = HUB_FILLET
c45 = math.cos(math.pi / 4)
prof = (cq.Workplane("XZ")
        .moveTo(0, 0)
        .lineTo(R_OUT, 0)
        .lineTo(R_OUT, T / 2 - GROOVE_R)
        .threePointArc((R_OUT - GROOVE_R, T / 2), (R_OUT, T / 2 + GROOVE_R))
        .lineTo(R_OUT, T)
        .lineTo(rh + f, T)
        .threePointArc((rh + f - f * c45, T + f - f * c45), (rh, T + f)))
if HUB_CHAMFER > 0:
    prof = (prof.lineTo(rh, T + HUB_H - HUB_CHAMFER)
            .lineTo(rh - HUB_CHAMFER, T + HUB_H))
else:
    prof = prof.lineTo(rh, T + HUB_H)
prof = prof.lineTo(0, T + HUB_H).close()
body = prof.revolve(360, (0, 0, 0), (0, 1, 0))
# put the revolve seam at the back so it does not streak the visible faces
body = body.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)

# ---------------- window cut-outs (4x) ----------------
half = SPOKE_W / 2.0
big = CUT_R + 10
box = cq.Workplane("XY").box(big, big, T * 3, centered=False).translate((half, half, -T))
cyl = cq.Workplane("XY").circle(CUT_R).extrude(T * 3).translate((0, 0, -T))
window = box.intersect(cyl)
yc = math.sqrt(CUT_R ** 2 - half ** 2)
window = window.edges("|Z").edges(cq.selectors.NearestToPointSelector((half, half, 0))).fillet(CUT_FILLET_IN)
window = window.edges(cq.selectors.NearestToPointSelector((half, yc, 0))).fillet(CUT_FILLET_OUT)
window = window.edges(cq.selectors.NearestToPointSelector((yc, half, 0))).fillet(CUT_FILLET_OUT)
for i in range(4):
    body = body.cut(window.rotate((0, 0, 0), (0, 0, 1), 90 * i))

# ---------------- spline bore ----------------
pts = []
n = SPL_TEETH
for k in range(2 * n):
    a = math.pi * k / n
    r = SPL_MAJOR / 2 if k % 2 == 0 else SPL_MINOR / 2
    pts.append((r * math.cos(a), r * math.sin(a)))
spline = (cq.Workplane("XY").workplane(offset=T + HUB_H - SPL_DEPTH)
          .polyline(pts).close().extrude(SPL_DEPTH + 1))
body = body.cut(spline)

# ---------------- through hole ----------------
hole = cq.Workplane("XY").circle(HOLE_D / 2).extrude(T + HUB_H + 2).translate((0, 0, -1))
body = body.cut(hole)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
